import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 300.0          # outer length (X)
W = 100.0          # outer width (Y)
H = 10.9           # frame height
R_OUT = 2.8        # outer vertical corner radius
CH_H = 3.9         # top outer chamfer, horizontal run
CH_V = 4.5         # top outer chamfer, vertical rise
T = 9.2            # wall thickness (outer face -> inner face)
IC = 0.6           # small chamfer on the inner top edge (runs round the tabs too)
R_IN = 1.0         # small radius on the inner vertical corners
RB_H = 1.5         # rebate along the inner bottom edge: height
RB_D = 2.5         # rebate depth into the wall
LIP_Z = 2.7        # top of the narrow lip band just above the rebate
LIP_P = 0.4        # lip protrusion beyond the inner face

NOTCH_L = 5.8      # deeper pocket at each inner corner: length along each wall
NOTCH_H = 4.0      # pocket height from the bottom
NOTCH_D = 6.5      # pocket depth into the wall (from the inner face)

TAB_W = 18.4       # tab width along X
TAB_REACH = 29.3   # tab far edge measured from the front outer face
TAB_H = 7.9        # tab height (top flush with frame top)
TAB_X = 105.4      # tab centre distance from part centre along X

FOOT_LEN = 53.4    # strip under each end wall, length along Y
FOOT_W = 2.4       # strip width along X
FOOT_IN = 2.3      # strip inset from the end face
FOOT_H = 2.3       # strip height below the frame


def rrect(w, h, r):
    """Rounded rectangle sketch."""
    return cq.Sketch().rect(w, h).vertices().fillet(r)


def slab(w, h, r, z0, dz):
    """Rounded-rectangle prism from z0 up by dz."""
    return (
        cq.Workplane("XY")
        .workplane(offset=z0)
        .placeSketch(rrect(w, h, r))
        .extrude(dz)
    )


def box(x0, x1, y0, y1, z0, z1):
    """Axis-aligned block between the given coordinates."""
    return (
        cq.Workplane("XY")
        .workplane(offset=min(z0, z1))
        .center((x0 + x1) / 2, (y0 + y1) / 2)
        .rect(abs(x1 - x0), abs(y1 - y0))
        .extrude(abs(z1 - z0))
    )


# ---------------- outer body: rounded box with a chamfered top ----------------
body = slab(L, W, R_OUT, 0, H - CH_V)
cap = (
    cq.Workplane("XY")
    .workplane(offset=H - CH_V)
    .placeSketch(
        rrect(L, W, R_OUT),
        rrect(L - 2 * CH_H, W - 2 * CH_H, R_OUT).moved(
            cq.Location(cq.Vector(0, 0, CH_V))
        ),
    )
    .loft()
)
body = body.union(cap)

# ---------------- window through the frame ----------------
TL = T + LIP_P
body = body.cut(slab(L - 2 * TL, W - 2 * TL, R_IN, -1, H + 2))
body = body.cut(slab(L - 2 * T, W - 2 * T, R_IN, LIP_Z, H + 1))

# ---------------- two tabs standing off the front wall ----------------
y_in = -W / 2 + T
y_far = -W / 2 + TAB_REACH
for sx in (-1, 1):
    body = body.union(
        box(sx * TAB_X - TAB_W / 2, sx * TAB_X + TAB_W / 2, y_in - 0.5, y_far, H - TAB_H, H)
    )
body = body.clean()

# ---------------- small chamfer round the whole inner top contour ----------------
solid = body.val()
tops = [f for f in solid.Faces()
        if f.geomType() == "PLANE" and abs(f.Center().z - H) < 1e-6 and f.innerWires()]
if tops:
    top = max(tops, key=lambda f: f.Area())
    inner_edges = [e for w in top.innerWires() for e in w.Edges()]
    try:
        solid = solid.chamfer(IC, None, inner_edges)
    except Exception:
        pass  # keep the sharp inner edge if the kernel refuses the chamfer
body = cq.Workplane("XY").newObject([solid])

# ---------------- rebate along the inner bottom edge ----------------
body = body.cut(slab(L - 2 * (T - RB_D), W - 2 * (T - RB_D), R_IN, -1, RB_H + 1))

# ---------------- deeper pockets under each inner corner ----------------
EXT = 2.0  # overlap into the window so no slivers are left
for sx in (-1, 1):
    for sy in (-1, 1):
        xi = sx * (L / 2 - T)
        yi = sy * (W / 2 - T)
        # along the end wall
        body = body.cut(box(xi - sx * EXT, xi + sx * NOTCH_D,
                            yi - sy * NOTCH_L, yi + sy * NOTCH_D, -1, NOTCH_H))
        # along the long wall
        body = body.cut(box(xi - sx * NOTCH_L, xi + sx * NOTCH_D,
                            yi - sy * EXT, yi + sy * NOTCH_D, -1, NOTCH_H))

# ---------------- strips under the end walls ----------------
for sx in (-1, 1):
    x_out = sx * (L / 2 - FOOT_IN)
    x_in = sx * (L / 2 - FOOT_IN - FOOT_W)
    body = body.union(box(x_in, x_out, -FOOT_LEN / 2, FOOT_LEN / 2, -FOOT_H, 0.01))

result = body.clean()
VIEW = {"azimuth": 45, "elevation": 26}
